import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 300.0          # plate width  (X)
H = 185.5          # plate height (Z)
T = 4.2            # plate thickness (Y)
PLATE_R = 1.0      # plate corner radius
PLATE_BR = 2.0     # round-off on the back perimeter edges

# side brackets (thick tabs standing off the back of the plate)
BR_X = 123.2       # bracket centre distance from plate centre
BR_T = 9.5         # bracket thickness (X)
BR_H = 69.0        # bracket height (Z)
BR_D = 69.0        # bracket depth behind plate (Y)
BR_FIL = 9.0       # root fillet radius

SLOT_Y = 40.0      # slot centre distance from plate back
SLOT_L = 40.6      # slot overall length (along Y)
SLOT_W = 18.3      # slot width (Z)

PIN_D = 9.0        # stud diameter
PIN_L = 10.0       # stud length
PIN_P = 21.7       # stud pitch (Z)
PIN_CH = 0.4       # stud end chamfer (threads left out)

# centre U-channel (bent strip)
CH_W = 138.0       # outer width (X)
CH_D = 48.5        # outer depth behind plate (Y)
CH_H = 34.0        # strip height (Z)
CH_T = 5.0         # strip thickness
CH_RO = 6.5        # outer bend radius
CH_RI = 3.5        # inner bend radius
CH_FIL = 8.0       # root fillet radius


def junction_edges(solid, x0, x1, z0, z1, y=T, tol=1e-3):
    """Edges lying on the plate back face inside a footprint box."""
    out = []
    for e in solid.Edges():
        bb = e.BoundingBox()
        if abs(bb.ymin - y) < tol and abs(bb.ymax - y) < tol:
            if (bb.xmin > x0 - tol and bb.xmax < x1 + tol and
                    bb.zmin > z0 - tol and bb.zmax < z1 + tol):
                out.append(e)
    return out


# ---------------- plate ----------------
plate = (cq.Workplane("XY")
         .box(W, T, H)
         .translate((0, T / 2.0, 0))
         .edges("|Y").fillet(PLATE_R)
         .faces(">Y").edges().fillet(PLATE_BR))

body = plate

# ---------------- brackets ----------------
for sx in (-1, 1):
    xb = sx * BR_X
    br = (cq.Workplane("XY")
          .box(BR_T, BR_D, BR_H)
          .translate((xb, T + BR_D / 2.0, 0)))
    body = body.union(br)

# ---------------- U channel ----------------
outer = (cq.Workplane("XY")
         .box(CH_W, CH_D, CH_H)
         .translate((0, T + CH_D / 2.0, 0))
         .edges("|Z and >Y").fillet(CH_RO))
inner_d = CH_D - CH_T + 1.0
inner = (cq.Workplane("XY")
         .box(CH_W - 2 * CH_T, inner_d, CH_H + 2.0)
         .translate((0, T - 1.0 + inner_d / 2.0, 0))
         .edges("|Z and >Y").fillet(CH_RI))
channel = outer.cut(inner)
body = body.union(channel)

# ---------------- root fillets ----------------
solid = body.val()
edges = []
for sx in (-1, 1):
    xb = sx * BR_X
    edges += junction_edges(solid, xb - BR_T / 2, xb + BR_T / 2,
                            -BR_H / 2, BR_H / 2)
solid = solid.fillet(BR_FIL, edges)

edges = []
for sx in (-1, 1):
    x0 = sx * (CH_W / 2 - CH_T / 2)
    edges += [e for e in junction_edges(solid, x0 - CH_T / 2, x0 + CH_T / 2,
                                        -CH_H / 2, CH_H / 2)
              if e.BoundingBox().zlen > CH_H / 2]
solid = solid.fillet(CH_FIL, edges)
body = cq.Workplane("XY").add(solid)

# ---------------- slots & studs ----------------
for sx in (-1, 1):
    xb = sx * BR_X
    slot = (cq.Workplane("YZ", origin=(xb - BR_T, 0, 0))
            .center(T + SLOT_Y, 0)
            .slot2D(SLOT_L, SLOT_W, 0)
            .extrude(2 * BR_T))
    body = body.cut(slot)
    for k in (-1, 0, 1):
        pin = (cq.Workplane("XZ", origin=(xb, T + BR_D, k * PIN_P))
               .circle(PIN_D / 2.0)
               .extrude(-PIN_L))
        if PIN_CH > 0:
            pin = pin.faces(">Y").edges().chamfer(PIN_CH)
        body = body.union(pin)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
